import cadquery as cq

# Router port bezel / frame: square thin-walled frame with an outer flange band,
# four mounting ears, notched lower walls, six RJ45 port dividers on the +X side
# and engraved port labels.

# ---------------- driving dimensions (mm) ----------------
B = 51.55          # half size of the outer flange band (square)
WO = 49.05         # half size of the wall outer face
WI = 47.6          # half size of the wall inner face
HB = 9.85          # flange band height
HU = 4.85          # upper wall height above band
D1 = 4.9           # lower wall depth below band (level 1)
D2 = 8.85          # deeper tab depth (level 2)
EAR_R = 3.9        # mounting ear radius
EAR_HOLE = 3.6     # mounting ear hole dia
SIDE_HOLE = 7.0    # side hole dia (through +/-Y band)
SIDE_HOLE_X = 14.7
SIDE_HOLE_Z = 5.3
LIP_D = 2.8        # +X wall lip below band between the ports
FIN_T = 3.3        # port divider thickness
FIN_X_IN = 26.5    # x of the inner end of dividers
FIN_D = 15.5       # end divider depth below band
FIN_D_MID = 15.5   # inner dividers depth below band
FIN_R = 1.5        # rounding of the divider bottom edges facing the ports
FIN_Z_IN = -3.35   # top of the divider inner end (45-ish deg slope from wall top)
FOOT_D = 17.05     # divider foot depth
FOOT_L = 2.8       # foot length
N_FIN = 6
PITCH = 2 * WI / (N_FIN - 1)
TEXT_H = 5.75      # font size (cap height ~4.35)
TEXT_Z = 3.4       # label centre height above band bottom
TEXT_DEPTH = 0.6      # engraving depth
LABELS = ["WAN0", "LAN0", "LAN1", "LAN2", "LAN3"]

ZTOP = HB + HU


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- flange band + upper wall ----------------
band = (cq.Workplane("XY").rect(2 * B, 2 * B).rect(2 * WI, 2 * WI)
        .extrude(HB))
upper = (cq.Workplane("XY").workplane(offset=HB)
         .rect(2 * WO, 2 * WO).rect(2 * WI, 2 * WI).extrude(HU))
body = band.union(upper)

# ---------------- mounting ears ----------------
# left ears stick out in -X, right ears stick out in +/-Y
def ear_solid(cx, cy, rx0, rx1, ry0, ry1):
    c = cq.Workplane("XY").center(cx, cy).circle(EAR_R).extrude(HB)
    r = box(rx0, rx1, ry0, ry1, 0, HB)
    return c.union(r)

ear_list = []
# (-X,+Y) and (-X,-Y)
for sy in (1, -1):
    cy = sy * (B - EAR_R)
    ear_list.append(((-B - EAR_R, cy),
                     ear_solid(-B - EAR_R, cy, -B - EAR_R, -B + 0.5,
                               cy - EAR_R, cy + EAR_R)))
# (+X,+Y) and (+X,-Y)
for sy in (1, -1):
    cx = B - EAR_R
    cy = sy * (B + EAR_R)
    y0, y1 = sorted((cy, sy * (B - 0.5)))
    ear_list.append(((cx, cy),
                     ear_solid(cx, cy, cx - EAR_R, cx + EAR_R, y0, y1)))

for (cx, cy), e in ear_list:
    body = body.union(e)
for (cx, cy), e in ear_list:
    body = body.cut(cq.Workplane("XY").center(cx, cy)
                    .circle(EAR_HOLE / 2).extrude(HB))

# ---------------- lower walls / tabs ----------------
# -X wall, level 1, with notches (to band bottom)
lowx = box(-WO, -WI, -WO, WO, -D1, 0)
for y0, y1 in ((15.55, 28.8), (-3.55, 1.0), (-14.5, -10.4)):
    lowx = lowx.cut(box(-WO - 1, -WI + 1, y0, y1, -D1 - 1, 0))
body = body.union(lowx)

# +Y wall, level 1 with a notch, plus a deeper tab flush with the band
lowy = box(-WO, WO, WI, WO, -D1, 0)
lowy = lowy.cut(box(-35.9, -27.25, WI - 1, WO + 1, -D1 - 1, 0))
body = body.union(lowy)
body = body.union(box(8.7, 23.4, WI, B, -D2, 0))

# +X wall lip below the band (top edge of the port openings)
body = body.union(box(WI, B, -WI, WI, -LIP_D, 0))

# -Y wall tabs (level 1)
for x0, x1 in ((-WO, -45.0), (-32.85, -25.1), (3.1, WO)):
    body = body.union(box(x0, x1, -WO, -WI, -D1, 0))

# ---------------- port dividers (fins) ----------------
# profile in XZ: ~40 deg sloped top from the wall top, vertical inner end,
# bottom with a small foot at the outer (+X) end
def fin_profile(depth):
    return [
        (WI, ZTOP),
        (FIN_X_IN, FIN_Z_IN),
        (FIN_X_IN, -depth),
        (B - FOOT_L, -depth),
        (B - FOOT_L, -FOOT_D),
        (B, -FOOT_D),
        (B, 0),
        (WI, 0),
    ]


for i in range(N_FIN):
    yc = -WI + i * PITCH
    fin_pts = fin_profile(FIN_D if i in (0, N_FIN - 1) else FIN_D_MID)
    y0 = max(yc - FIN_T / 2, -WO)
    y1 = min(yc + FIN_T / 2, WO)
    fin = (cq.Workplane("XZ", origin=(0, y1, 0))
           .polyline(fin_pts).close().extrude(y1 - y0))
    if FIN_R > 0:
        # round the bottom edges facing the port openings
        d = FIN_D if i in (0, N_FIN - 1) else FIN_D_MID
        ya = y0 - 0.2 if i > 0 else y1 - 0.2
        yb = y1 + 0.2 if i < N_FIN - 1 else y0 + 0.2
        fin = fin.edges(cq.selectors.BoxSelector(
            (FIN_X_IN + 0.2, ya, -d - 0.2),
            (B - FOOT_L - 0.2, yb, -d + 0.2))).fillet(FIN_R)
    body = body.union(fin)

# ---------------- side holes through the +/-Y band ----------------
for sy in (1, -1):
    y_start = sy * (WI - 1.0) if sy > 0 else -(B + 1.0)
    h = cq.Workplane("XY").add(cq.Solid.makeCylinder(
        SIDE_HOLE / 2, B - WI + 2.0,
        cq.Vector(SIDE_HOLE_X, y_start, SIDE_HOLE_Z), cq.Vector(0, 1, 0)))
    body = body.cut(h)

# ---------------- engraved port labels on the +X face ----------------
for i, lab in enumerate(LABELS):
    yc = -WI + (i + 0.5) * PITCH
    pl = cq.Plane(origin=(B, yc, TEXT_Z), xDir=(0, 1, 0), normal=(1, 0, 0))
    txt = cq.Workplane(pl).text(lab, TEXT_H, -TEXT_DEPTH, combine=False)
    body = body.cut(txt)

result = body
